import math
import cadquery as cq

# =====================================================================
# Lower housing tray with loose hinge strip and thumb-wheel knob.
# Tray: X = length, Y = depth (front at -Y, open back at +Y), Z = up.
# =====================================================================

# ---------------- tray driving dimensions (mm) ----------------
L = 150.0            # tray length (X) at the top edge of the body
W = 55.8             # tray depth (Y) at the top edge of the body
HB = 19.0            # body height (below the lip)
HL = 4.2             # lip height
DRAFT = 12.0         # draft of front / end faces (deg), outer and inner
R_TOPC = 5.5         # plan radius of the front corners at the body top
R_OUT = 8.5          # outer bottom blend radius
LIP_IN_X = 1.8       # lip outer face inset from the body top edge at the ends
LIP_IN_Y = 1.5       # lip outer face inset from the body top edge at the front
LIP_R = 0.35         # lip top edge rounding
WALL_X = 2.6         # inner wall inset (lip inner face) from the body top edge, ends
WALL_Y = 3.0         # inner wall inset (lip inner face) from the body top edge, front
Z_LIPIN = 18.5       # inner wall is vertical above this height
R_IN = 6.5           # inner bottom blend radius
T_FLOOR = 3.0        # floor thickness
FLOOR_BACK = 3.0     # floor stops this far short of the back plane
FLOOR_CUT_X = 67.0   # half width of the floor cut at the back

# hinge seat along the back edge of the floor
SEAT_HALF = 41.1
SEAT_Y0 = 16.8
SEAT_DEPTH = 1.35

# button pad (left end)
PAD_X0, PAD_X1 = -41.9, -12.4
PAD_Y0, PAD_Y1 = -19.4, 7.7
PAD_DEPTH = 1.5      # button pad is a shallow pocket in the floor
BTN_X0, BTN_X1 = -31.2, -21.8
BTN_H = 5.5
BTN_Y = [2.05, -5.96, -13.9]
BUMP_X = [-36.5, -16.3]
BUMP_Y = [2.0, -6.1, -14.1]
BUMP_D = 2.8
BUMP_H = 1.0

# round hole (left end)
HOLE_X, HOLE_Y, HOLE_D = -57.8, -11.4, 8.7

# stepped display window (right end)
WIN_X0, WIN_X1 = 35.4, 58.7          # through opening
WIN_Y0, WIN_Y1 = -20.2, 13.1
REB_X0, REB_X1 = 27.9, 64.6          # rebate (ledges on both X sides)
Z_REB = 1.4                          # ledge height
POST_X = [30.8, 62.1]
POST_Y = [10.5, -17.4]
POST_D = 3.4
POST_TOP = 5.3
SLOT_X0, SLOT_X1 = 61.3, 64.4
SLOT_Y0, SLOT_Y1 = -9.5, 2.7

# shelf bracket on the inside of the left end wall
BR_X1 = -66.0
BR_Y0, BR_Y1 = -20.4, 9.0
BR_Z0, BR_Z1 = 17.2, 20.2
BR_HOLES = [0.9, -16.2]
BR_HOLE_X = -69.1

# snap catches on the inside of the front lip
# (x0, x1, z0, z1, inner face y) of each catch
CATCH_SPANS = [(-66.0, -46.7, 17.8, 20.3, -20.8), (-13.4, 13.3, 18.0, 22.6, -21.4)]

# ---------------- hinge strip (separate body behind the tray) ----------------
HG_LEN = 82.0
HG_Y0 = 47.3          # plate front edge (between knuckles)
HG_Y1 = 55.45         # plate back edge
HG_T = 1.3
KN_OD = 5.8
KN_ID = 2.7
KN_Y = 45.35
KN_LEN = 11.6
KN_X = [-35.3, -11.75, 11.75, 35.3]

# ---------------- knob (separate body in front of the tray) ----------------
KB_D = 26.6
KB_T = 4.0
KB_X = -12.9
KB_Y = -49.1
KB_DR = 4.3           # D-pocket radius
KB_DFLAT = 2.6        # D-pocket flat offset (toward +Y)
KB_DDEPTH = 2.0


def plan(x_half, y_front, y_back, rc):
    """Rounded rectangle in XY (all corners radius rc); the back corners are cut away later."""
    rc = max(rc, 0.3)
    return (
        cq.Workplane("XY")
        .center(0, (y_front + y_back) / 2.0)
        .sketch()
        .rect(2 * x_half, y_back - y_front)
        .vertices()
        .fillet(rc)
        .finalize()
    )


def tapered(x_half_top, y_front_top, rc_top, z0, z1, draft_deg, y_back):
    """Solid from z0 to z1 whose sides lean outward going up by draft_deg (plan given at the top)."""
    d = (z1 - z0) * math.tan(math.radians(draft_deg))
    bot = plan(x_half_top - d, y_front_top + d, y_back - d, rc_top - d)
    return bot.extrude(z1 - z0, taper=-draft_deg).translate((0, 0, z0))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


YB_EXT = W / 2.0 + 40.0
ZTOP = HB + HL

# ---------------- outer body with lip ----------------
outer = tapered(L / 2.0, -W / 2.0, R_TOPC, 0.0, HB, DRAFT, YB_EXT)
outer = outer.faces("<Z").edges().fillet(R_OUT)
lip = plan(L / 2.0 - LIP_IN_X, -W / 2.0 + LIP_IN_Y, YB_EXT, R_TOPC - LIP_IN_Y).extrude(HL).translate((0, 0, HB))
body = outer.union(lip)

# ---------------- cavity (open top and open back) ----------------
cav_low = tapered(L / 2.0 - WALL_X, -W / 2.0 + WALL_Y, R_TOPC - WALL_Y, T_FLOOR, Z_LIPIN, DRAFT, YB_EXT)
cav_low = cav_low.faces("<Z").edges().fillet(R_IN)
cav_up = plan(L / 2.0 - WALL_X, -W / 2.0 + WALL_Y, YB_EXT, R_TOPC - WALL_Y).extrude(ZTOP + 2 - Z_LIPIN).translate(
    (0, 0, Z_LIPIN)
)
body = body.cut(cav_low).cut(cav_up)

# flat back
body = body.cut(box(-L, L, W / 2.0, W / 2.0 + 80, -10, 40))

# soften the top edges of the lip
lip_top_edges = [e for e in body.faces(">Z").edges().vals() if e.Center().y < W / 2.0 - 0.5]
body = body.newObject(lip_top_edges).fillet(LIP_R)

# floor stops short of the back plane
body = body.cut(box(-FLOOR_CUT_X, FLOOR_CUT_X, W / 2.0 - FLOOR_BACK, W / 2.0 + 1, -1, T_FLOOR + 5.0))

# hinge seat (shallow rebate along the back edge)
body = body.cut(box(-SEAT_HALF, SEAT_HALF, SEAT_Y0, W / 2.0 + 1, T_FLOOR - SEAT_DEPTH, T_FLOOR + 1))

# ---------------- button pad with three key slots and locating bumps ----------------
body = body.cut(box(PAD_X0, PAD_X1, PAD_Y0, PAD_Y1, T_FLOOR - PAD_DEPTH, T_FLOOR + 1))
for by in BUMP_Y:
    for bx in BUMP_X:
        body = body.union(
            cq.Workplane("XY").circle(BUMP_D / 2.0).extrude(BUMP_H + 0.2)
            .translate((bx, by, T_FLOOR - PAD_DEPTH - 0.2))
        )
for yc in BTN_Y:
    slot = (
        cq.Workplane("XY")
        .center((BTN_X0 + BTN_X1) / 2.0, yc)
        .rect(BTN_X1 - BTN_X0, BTN_H)
        .extrude(10)
        .edges("|Z")
        .fillet(0.8)
        .translate((0, 0, -2))
    )
    body = body.cut(slot)

# round through hole
body = body.cut(cq.Workplane("XY").circle(HOLE_D / 2.0).extrude(10).translate((HOLE_X, HOLE_Y, -2)))

# ---------------- stepped window with corner posts ----------------
body = body.cut(box(REB_X0, REB_X1, WIN_Y0, WIN_Y1, Z_REB, T_FLOOR + 1))
body = body.cut(box(WIN_X0, WIN_X1, WIN_Y0, WIN_Y1, -1, T_FLOOR + 1))
for px in POST_X:
    for py in POST_Y:
        body = body.union(
            cq.Workplane("XY").circle(POST_D / 2.0).extrude(POST_TOP - Z_REB + 0.1).translate((px, py, Z_REB - 0.1))
        )
# small pilot holes under the front posts
for px in POST_X:
    body = body.cut(cq.Workplane("XY").circle(1.2).extrude(2.5).translate((px, POST_Y[1], -0.5)))
# locating slot in the right ledge
slot = (
    cq.Workplane("XY")
    .center((SLOT_X0 + SLOT_X1) / 2.0, (SLOT_Y0 + SLOT_Y1) / 2.0)
    .slot2D(SLOT_Y1 - SLOT_Y0, SLOT_X1 - SLOT_X0, angle=90)
    .extrude(1.0)
    .translate((0, 0, Z_REB - 0.5))
)
body = body.cut(slot)

# ---------------- shelf bracket on the left end wall ----------------
bracket = box(-L / 2.0 + 1.0, BR_X1, BR_Y0, BR_Y1, BR_Z0, BR_Z1).edges("|Y").edges(">X").edges("<Z").fillet(1.0)
for hy in BR_HOLES:
    bracket = bracket.cut(cq.Workplane("XY").circle(0.8).extrude(10).translate((BR_HOLE_X, hy, BR_Z0 - 2)))
body = body.union(bracket)

# ---------------- snap catches inside the front lip ----------------
for x0, x1, cz0, cz1, cy in CATCH_SPANS:
    ramp = 1.2
    catch = (
        cq.Workplane("XZ")
        .polyline([(x0, cz0), (x1, cz0), (x1 - ramp, cz1), (x0 + ramp, cz1)])
        .close()
        .extrude(-(cy - (-W / 2.0 + WALL_Y - 0.3)))
        .translate((0, -W / 2.0 + WALL_Y - 0.3, 0))
    )
    body = body.union(catch)

tray = body

# ---------------- hinge strip ----------------
hinge = box(-HG_LEN / 2.0, HG_LEN / 2.0, HG_Y0, HG_Y1, 0, HG_T)
for kx in KN_X:
    kn = (
        cq.Workplane("YZ")
        .workplane(offset=kx - KN_LEN / 2.0)
        .center(KN_Y, KN_OD / 2.0)
        .circle(KN_OD / 2.0)
        .circle(KN_ID / 2.0)
        .extrude(KN_LEN)
    )
    hinge = hinge.union(kn)
for kx in KN_X:
    hinge = hinge.cut(
        cq.Workplane("YZ")
        .workplane(offset=kx - KN_LEN / 2.0 - 1)
        .center(KN_Y, KN_OD / 2.0)
        .circle(KN_ID / 2.0)
        .extrude(KN_LEN + 2)
    )

# ---------------- knob ----------------
knob = cq.Workplane("XY").circle(KB_D / 2.0).extrude(KB_T)
dpocket = (
    cq.Workplane("XY")
    .circle(KB_DR)
    .extrude(KB_DDEPTH + 1)
    .cut(box(-10, 10, KB_DFLAT, 10, -1, 10))
    .translate((0, 0, KB_T - KB_DDEPTH))
)
knob = knob.cut(dpocket).translate((KB_X, KB_Y, 0))

result = tray.union(hinge).union(knob)
